# Half of a vaned nozzle / guide-vane ring: a half-cylindrical shroud with three
# bolting lugs, two split flanges with bolt holes, and twisted cambered vanes
# standing on the inside of the shroud (free inner ends, flat hub faces).
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0        # outer radius of shroud
WALL = 5.0           # shroud wall thickness
R_IN = R_OUT - WALL  # inner radius of shroud
H = 47.5             # shroud height (axial)

# lugs (bolting tabs on the outside of the shroud)
LUG_ANGLES = [120.0, 180.0, 240.0]
LUG_R = 23.5         # lug outline radius
LUG_CR = 100.7       # radial position of lug outline centre
LUG_T = 12.0         # lug thickness (centred at mid-height)
LUG_HOLE_D = 11.3
LUG_HOLE_R = 110.0   # radial position of lug hole

# split flanges (ears at both ends of the half ring)
FL_T = 6.0           # flange thickness (x from -FL_T to 0)
FL_HOLE_D = 5.0
FL_HOLE_R = 109.5
FL_HOLE_DZ = 12.0    # hole offset from mid-height

# vanes
N_BLADES = 24        # vanes of the complete ring (sets the pitch)
N_HALF = 13          # vanes actually present in this half ring
H_B = 22.5           # vane axial height (from bottom)
LE_ANG = 86.5        # angular position of a vane leading edge (deg)
# vane sections lie in planes normal to the radial line through the LE:
# (distance of section plane from axis, LE->TE angular span in deg)
# the first one is the flat free (hub) end of the vane
SECTIONS = [(44.5, 24.5), (72.0, 21.3), (98.5, 16.3)]
R_TIP_CLIP = R_IN + WALL / 2.0   # vanes are buried half-way into the wall
TURN_DEG = 30.0      # camber turning (LE more tangential than TE)
T_MAX = 4.0          # max vane thickness
R_LE = 1.9           # leading edge radius
T_TE = 0.6           # trailing edge thickness
Z_LE = 1.9           # height of leading edge circle centre


def vane_profile(d, span_deg):
    """2D (u,z) construction data of a vane section in its plane.
    LE (round) at bottom at u=0, thin TE at top displaced toward +u."""
    L = (0.0, Z_LE)
    T = (d * math.tan(math.radians(span_deg)), H_B - 0.05)
    chord = math.hypot(T[0] - L[0], T[1] - L[1])
    gam = math.atan2(T[0] - L[0], T[1] - L[1])  # chord angle from +z toward +u
    turn = math.radians(TURN_DEG)
    rc = chord / (2.0 * math.sin(abs(turn) / 2.0))
    b0 = gam + turn / 2.0  # tangent angle at LE

    def tang(s):
        a = b0 - turn * s
        return (math.sin(a), math.cos(a))

    t0 = tang(0.0)
    C = (L[0] - t0[1] * rc, L[1] + t0[0] * rc)

    def cam(s):
        t = tang(s)
        return (C[0] + t[1] * rc, C[1] - t[0] * rc)

    def off(s, h):
        # point offset by h along the left normal of the camber line
        p = cam(s)
        t = tang(s)
        return (p[0] - t[1] * h, p[1] + t[0] * h)

    # thickness distribution (station, thickness)
    dist = [(0.07, 1.85 * R_LE), (0.3, T_MAX), (0.65, 0.62 * T_MAX)]
    ss = [off(1.0, T_TE / 2.0)] + [off(st, th / 2.0) for st, th in reversed(dist)]
    tip = (cam(0.0)[0] - t0[0] * R_LE, cam(0.0)[1] - t0[1] * R_LE)
    ps = [off(st, -th / 2.0) for st, th in dist] + [off(1.0, -T_TE / 2.0)]
    n0 = (-t0[1], t0[0])
    t1 = tang(1.0)
    return ss, tip, ps, (-n0[0], -n0[1]), t1


def vane_wire(d, le_deg, span_deg):
    a = math.radians(le_deg)
    er = cq.Vector(math.cos(a), math.sin(a), 0)
    et = cq.Vector(-math.sin(a), math.cos(a), 0)
    pl = cq.Plane(origin=er * d, xDir=et, normal=er)
    ss, tip, ps, tl, t1 = vane_profile(d, span_deg)
    w = (cq.Workplane(pl)
         .moveTo(*ss[0])
         .spline(ss[1:] + [tip], tangents=[(-t1[0], -t1[1]), tl], includeCurrent=True)
         .spline(ps, tangents=[tl, t1], includeCurrent=True)
         .close())
    return w.val()


def make_vane(le_deg):
    wires = [vane_wire(r, le_deg, sp) for (r, sp) in SECTIONS]
    return cq.Solid.makeLoft(wires, False)


# ---------------- shroud (half ring, x <= 0) ----------------
half_box = cq.Workplane("XY").box(400, 400, 200, centered=(False, True, True)).translate((-400, 0, 0))

shroud = (cq.Workplane("XY").circle(R_OUT).circle(R_IN).extrude(H))
shroud = shroud.intersect(half_box)

# ---------------- lugs ----------------
for a in LUG_ANGLES:
    ar = math.radians(a)
    cx, cy = LUG_CR * math.cos(ar), LUG_CR * math.sin(ar)
    hx, hy = LUG_HOLE_R * math.cos(ar), LUG_HOLE_R * math.sin(ar)
    lug = (cq.Workplane("XY").workplane(offset=H / 2.0 - LUG_T / 2.0)
           .center(cx, cy).circle(LUG_R).extrude(LUG_T))
    lug = lug.cut(cq.Workplane("XY").circle(R_IN).extrude(H))
    shroud = shroud.union(lug)
    hole = (cq.Workplane("XY").center(hx, hy).circle(LUG_HOLE_D / 2.0).extrude(H))
    shroud = shroud.cut(hole)

# ---------------- vanes ----------------
annulus = cq.Workplane("XY").circle(R_TIP_CLIP).extrude(H_B + 1.0)
clip = annulus.intersect(half_box)

pitch = 360.0 / N_BLADES
vanes = None
for k in range(N_HALF):
    th = LE_ANG + k * pitch
    v = cq.Workplane("XY").add(make_vane(th))
    v = v.intersect(clip)
    if not v.solids().vals():
        continue
    vanes = v if vanes is None else vanes.union(v)

# ---------------- split flanges ----------------
ears = []
for sgn in (1.0, -1.0):
    # profile in the YZ plane: radial coordinate along sgn*Y
    if sgn > 0:
        pl = cq.Plane(origin=(-FL_T, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    else:
        pl = cq.Plane(origin=(0, 0, 0), xDir=(0, -1, 0), normal=(-1, 0, 0))
    ear = (cq.Workplane(pl)
           .moveTo(R_IN, 0)
           .lineTo(R_OUT, 0)
           .threePointArc((R_OUT + H / 2.0, H / 2.0), (R_OUT, H))
           .lineTo(R_IN, H)
           .close()
           .extrude(FL_T))
    for dz in (-FL_HOLE_DZ, FL_HOLE_DZ):
        h = (cq.Workplane(pl).center(FL_HOLE_R, H / 2.0 + dz)
             .circle(FL_HOLE_D / 2.0).extrude(FL_T))
        ear = ear.cut(h)
    ears.append(ear)

body = shroud.union(vanes)
# flanges are fused without face merging so the flange stays a distinct face
for ear in ears:
    body = body.union(ear, clean=False)

result = body
